import math
import cadquery as cq

# --- driving dimensions (mm) ---
R_OUT = 60.0          # outer radius
H = 18.5              # overall height
BOT_CH_V = 6.45       # bottom chamfer vertical size
BOT_CH_H = 4.3        # bottom chamfer horizontal size
BOT_FILLET = 3.5      # blend between outer cylinder and bottom chamfer
RIM_W = 5.0           # rim (wall) thickness at top
POCKET_D = 12.7       # depth from rim top to floor
IN_CH = 4.25          # 45 deg chamfer between inner wall and floor
SLOT_W = 6.0
SLOT_L = 42.5
SLOT_OFF = 12.0       # slot centre offset from axis (x)
SLOT_D = 3.3
SEAM_ANGLE = 45.0     # cosmetic: angular position of the revolve seam

R_IN = R_OUT - RIM_W
Z_FLOOR = H - POCKET_D

# fillet geometry for the cylinder / chamfer corner
alpha = math.atan2(BOT_CH_H, BOT_CH_V)          # chamfer angle from vertical
t = BOT_FILLET * math.tan(alpha / 2.0)          # tangent length
p_chamf = (R_OUT - t * math.sin(alpha), BOT_CH_V - t * math.cos(alpha))
p_cyl = (R_OUT, BOT_CH_V + t)
ctr = (R_OUT - BOT_FILLET, BOT_CH_V + t)
p_mid = (ctr[0] + BOT_FILLET * math.cos(alpha / 2.0),
         ctr[1] - BOT_FILLET * math.sin(alpha / 2.0))

# half cross-section in the XZ plane (local x = radius, local y = height)
prof = (
    cq.Workplane("XZ")
    .moveTo(0, 0)
    .lineTo(R_OUT - BOT_CH_H, 0)
    .lineTo(*p_chamf)
    .threePointArc(p_mid, p_cyl)
    .lineTo(R_OUT, H)
    .lineTo(R_IN, H)
    .lineTo(R_IN, Z_FLOOR + IN_CH)
    .lineTo(R_IN - IN_CH, Z_FLOOR)
    .lineTo(0, Z_FLOOR)
    .close()
)
# revolve, then turn the body so the revolve seam sits on a view silhouette
body = prof.revolve(360, (0, 0, 0), (0, 1, 0)).rotate((0, 0, 0), (0, 0, 1), SEAM_ANGLE)

slots = (
    cq.Workplane("XY").workplane(offset=Z_FLOOR)
    .pushPoints([(-SLOT_OFF, 0), (SLOT_OFF, 0)])
    .rect(SLOT_W, SLOT_L)
    .extrude(-SLOT_D)
)
result = body.cut(slots)

VIEW = {"azimuth": 45, "elevation": 26}
